import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 118.0            # overall length, back (x=0) to face (x=L)
HW = 37.6            # max half width of head / lid
LID_Z0 = 56.0        # lid lower edge
LID_TOP_BACK = 74.0  # lid top at the back
LID_TOP_FRONT = 78.4 # lid top where the head starts
HEAD_XB = 81.0       # back of head block
HEAD_X0 = 97.2       # back of the raised head (top)
HEAD_PEAK_X = 103.4
HEAD_TOP = 89.6      # top of head
HEAD_CROWN_HW = 12.0 # flat crown half width
HEAD_SH_Z = 56.0     # shoulder curve starts at this height on the side
HEAD_SHOULDER = [(37.0, 65.0), (33.5, 73.0), (27.5, 80.0), (19.5, 86.3), (HEAD_CROWN_HW, HEAD_TOP)]
HEAD_CHIN_Z = 28.6   # chin chamfer meets the side here
HEAD_MID_R = 14.0
HEAD_BOT_HW = 13.0   # chin half width ...
HEAD_BOT_Z = 5.0     # ... at this height
HEAD_FRONT_R = 12.0  # rounding of the face edges
LID_CUT_X = 85.0     # lid is trimmed to the helmet section from here on
BACK_CH = 5.5        # back top chamfer (x) ...
BACK_CH_Z = 66.5     # ... down to this height on the back wall
BACK_BOT_Z = 19.0    # bottom of back wall
BOT_FLAT_X0 = 42.0   # start of flat bottom
SIDE_INSET = 1.5     # lower body inset under the lid
SIDE_PANEL_D = 0.7   # depth of the stepped panel on the back box sides
LOW_HW0 = 18.5       # half width of the body bottom (z=0)
LOW_HW1 = 21.5       # half width of the body at z=14
LID_BEV_Z = 63.5     # lid side bevel starts here
LID_BEV_ANG = 32.0   # lid side bevel angle (deg from vertical)

TAPER_X1 = 58.0      # plan taper ends here
BACK_HW = 19.4       # half width of the back end
BACK_PLAN_R = 6.0

WIN_X0, WIN_X1 = 41.0, 77.0   # tunnel (window) extent in x
WIN_Z0, WIN_Z1 = 13.0, 55.0   # tunnel extent in z
WIN_CH = 8.0                  # front-bottom corner chamfer of tunnel
WIN_R_BACK = 10.0             # back-bottom corner radius of tunnel
FRAME_PTS = [(34.85, 56.0), (34.85, 22.0), (42.0, 4.0), (75.0, 4.0), (80.8, 17.8), (80.8, 56.0)]
                              # outline of the raised frame around the window
FRAME_D = 1.6                 # window frame inner step depth
FRAME_LIP = 2.0               # window frame inner step width

PIVOT_X, PIVOT_Z = 91.5, 56.5 # ear pivot centre
HUB_R = 9.2                   # ear hub circumradius (octagon)
ARM_Y0, ARM_T = 37.9, 4.4     # ear inner face |y| and thickness
HUB_T = 6.0
STRAP_T = 2.0                 # raised strap below the hub

GRIP_X, GRIP_Z, GRIP_L, GRIP_H, GRIP_Y = 56.0, 68.8, 14.0, 5.0, 32.8

HANDLE_X0, HANDLE_W = 35.5, 5.0
HANDLE_HY = 24.0
HANDLE_TOP = 86.5
HANDLE_LEG = 4.5
HANDLE_BAR = 3.5
HANDLE_R = 10.0

FOOT_X, FOOT_W, FOOT_HY, FOOT_H = 57.5, 17.0, 27.0, 6.0

FACE_W, FACE_H, FACE_ZC = 52.0, 37.0, 56.0
FACE_R, FACE_D = 6.0, 2.0
EYE_W, EYE_H, EYE_Y, EYE_CH, EYE_UP = 9.5, 18.5, 12.5, 2.8, 0.6
EYE_TAPER, EYE_X_START, EYE_FLOOR_X = 35.0, 110.0, 115.8
EYE_ZC = 55.5

CEIL_X, CEIL_R, CEIL_H = 62.0, 11.5, 3.0   # round boss on the tunnel ceiling
DISC_X, DISC_R, DISC_H = 89.0, 10.3, 2.0

VIEW = {"azimuth": 45, "elevation": 26}

BIG = 400.0


def lid_top_z(x):
    return LID_TOP_BACK + (LID_TOP_FRONT - LID_TOP_BACK) * (x - BACK_CH) / (HEAD_X0 - BACK_CH)


def plan_solid(off=0.0):
    """tapered plan outline extruded through z (offset inwards by off)"""
    pts = [(0, -(BACK_HW - off)), (TAPER_X1, -(HW - off)), (L + 20, -(HW - off)),
           (L + 20, HW - off), (TAPER_X1, HW - off), (0, BACK_HW - off)]
    return cq.Workplane("XY").polyline(pts).close().extrude(BIG / 2, both=True)


# ---------------- back body (lid + lower box + tunnel frame) ----------------
back_side = (
    cq.Workplane("XZ")
    .moveTo(0, BACK_BOT_Z)
    .lineTo(BOT_FLAT_X0, 0.0)
    .lineTo(77.0, 0.0)
    .lineTo(84.6, 9.4)
    .lineTo(84.6, LID_Z0)
    .lineTo(HEAD_X0 + 3, LID_Z0)
    .lineTo(HEAD_X0 + 3, lid_top_z(HEAD_X0 + 3))
    .lineTo(BACK_CH, LID_TOP_BACK)
    .lineTo(0.0, BACK_CH_Z)
    .close()
    .extrude(BIG / 2, both=True)
)


def lid_plan():
    """tapered plan outline; the lid sides are bevelled inwards above LID_BEV_Z"""
    pts = [(0, -BACK_HW), (TAPER_X1, -HW), (L + 20, -HW), (L + 20, HW), (TAPER_X1, HW), (0, BACK_HW)]
    sk = cq.Sketch().polygon(pts + [pts[0]]).vertices("<X").fillet(BACK_PLAN_R)
    low = cq.Workplane("XY").workplane(offset=-20).placeSketch(sk).extrude(LID_BEV_Z + 20)
    up = (cq.Workplane("XY").workplane(offset=LID_BEV_Z).placeSketch(sk.copy())
          .extrude(30, taper=LID_BEV_ANG))
    return low.union(up)


back = back_side.intersect(lid_plan())

# lower narrowing of the tunnel frame / box bottom (cross section)
low_cs = (
    cq.Workplane("YZ")
    .polyline([(-LOW_HW0, -5), (LOW_HW0, -5), (LOW_HW0, 0), (LOW_HW1, 14.0), (HW + 2, 34),
               (HW + 2, 200), (-HW - 2, 200), (-HW - 2, 34), (-LOW_HW1, 14.0), (-LOW_HW0, 0)])
    .close()
    .extrude(BIG / 2, both=True)
)
back = back.intersect(low_cs)

# lower body inset below the lid
lower_zone = (cq.Workplane("XY").box(84.6 + 10, BIG, LID_Z0 + 10, centered=(False, True, False))
              .translate((-10, 0, -10)))
back = back.cut(lower_zone.cut(plan_solid(SIDE_INSET)))


# ---------------- head ----------------
def head_prism(g=0.0, xf=None, front_r=0.0):
    """helmet cross-section (flat crown, sloped shoulders, chamfered chin) extruded along x"""
    xf = L + 10 if xf is None else xf
    ky = 1.0 + g / HW
    kz = 1.0 + g / (HEAD_TOP - 50.0)
    P = lambda y, z: (y * ky, 50.0 + (z - 50.0) * kz)
    sh = [P(*p) for p in HEAD_SHOULDER]
    w = (cq.Workplane("YZ")
         .moveTo(*P(-HEAD_BOT_HW, HEAD_BOT_Z))
         .lineTo(*P(HEAD_BOT_HW, HEAD_BOT_Z))
         .lineTo(*P(HW, HEAD_CHIN_Z))
         .lineTo(*P(HW, HEAD_SH_Z))
         .spline(sh, tangents=[(0, 1), (-1, 0)], includeCurrent=True)
         .lineTo(*P(-HEAD_CROWN_HW, HEAD_TOP))
         .spline([(-y, z) for (y, z) in reversed(sh[:-1])] + [P(-HW, HEAD_SH_Z)],
                 tangents=[(-1, 0), (0, -1)], includeCurrent=True)
         .lineTo(*P(-HW, HEAD_CHIN_Z))
         .close())
    p = w.extrude(xf - HEAD_XB).translate((HEAD_XB, 0, 0))
    p = p.edges("|X").edges(cq.selectors.BoxSelector((-100, -100, 15), (200, 100, 40))).fillet(HEAD_MID_R)
    if front_r > 0:
        p = p.faces(">X").edges().fillet(front_r)
    return p


def head_side(dx=0.0):
    front = [(88.5, 10.9), (98.0, 12.25), (105.8, 16.1), (111.5, 21.0), (115.9, 27.6),
             (117.7, 38.0), (L, 48.0)]
    top = [(117.3, 61.5), (114.1, 76.5), (108.5, 85.3), (HEAD_PEAK_X, HEAD_TOP)]
    backs = [(101.6, 87.0), (99.8, 82.5), (97.8, 79.4)]
    sh = lambda pts: [(x + dx, z) for (x, z) in pts]
    w = (cq.Workplane("XZ")
         .moveTo(HEAD_XB - 5, -5)
         .lineTo(77.0 + dx, -5)
         .lineTo(77.0 + dx, 0.0)
         .lineTo(84.6 + dx, 9.4)
         .spline(sh(front), tangents=[(1, 0.15), (0, 1)], includeCurrent=True)
         .spline(sh(top), tangents=[(0, 1), (-1, 0)], includeCurrent=True)
         .spline(sh(backs), tangents=[(-1, 0), (-1, -0.15)], includeCurrent=True)
         .lineTo(LID_CUT_X + dx, lid_top_z(LID_CUT_X) + 0.15)
         .lineTo(HEAD_XB - 5, lid_top_z(HEAD_XB - 5) - 0.6)
         .close())
    return w.extrude(BIG / 2, both=True)


def head_shape(dx=0.0, g=0.0):
    return head_prism(g, L + dx + g, HEAD_FRONT_R).intersect(head_side(dx + g))


head = head_shape()
# the lid disappears into the helmet: trim it to the head section ahead of LID_CUT_X
trim = (cq.Workplane("XY").box(100, BIG, BIG, centered=(False, True, True))
        .translate((LID_CUT_X, 0, 0)).cut(head_prism()))
back = back.cut(trim)
body = back.union(head)

# ---------------- tunnel through the body (along Y) ----------------
def win_profile(wp, grow=0.0):
    """tunnel / window outline in the XZ plane: large rounded back-bottom corner,
    chamfered front-bottom corner"""
    x0, x1 = WIN_X0 - grow, WIN_X1 + grow
    z0, z1 = WIN_Z0 - grow, WIN_Z1 + grow
    r = WIN_R_BACK
    c = WIN_CH
    k = 1.0 - math.sqrt(0.5)
    return (wp.moveTo(x0, z1)
            .lineTo(x0, z0 + r)
            .threePointArc((x0 + r * k, z0 + r * k), (x0 + r, z0))
            .lineTo(x1 - c * 0.8, z0)
            .lineTo(x1, z0 + c * 0.8)
            .lineTo(x1, z1)
            .close())


tunnel = win_profile(cq.Workplane("XZ")).extrude(BIG / 2, both=True)
body = body.cut(tunnel)

# raised frame (flush with the lid side) around the window on both sides
rim = (cq.Workplane("XZ").polyline(FRAME_PTS).close().extrude(BIG / 2, both=True)
       .intersect(plan_solid(0.0)).intersect(low_cs)
       .intersect(cq.Workplane("XY").box(BIG, BIG, LID_Z0, centered=(True, True, False)))
       .cut(tunnel))
body = body.union(rim)
# small bevel step inside the opening
step = win_profile(cq.Workplane("XZ"), FRAME_LIP).extrude(BIG / 2, both=True)
body = body.cut(step.cut(plan_solid(FRAME_D)))

# ---------------- face panel recess and eyes ----------------
panel = (cq.Workplane("YZ").center(0, FACE_ZC).rect(FACE_W, FACE_H).extrude(40)
         .translate((100, 0, 0)).edges("|X").fillet(FACE_R))
body = body.cut(panel.cut(head_shape(-FACE_D)))


def eye(yc):
    # chamfered-rectangle eye pad with sloped (tapered) flanks, grown from below the
    # panel floor so that it meets the floor with its nominal outline
    d = (EYE_FLOOR_X - EYE_X_START) * math.tan(math.radians(EYE_TAPER))
    w, h = EYE_W + 2 * d, EYE_H + 2 * d
    c = EYE_CH + d * (1 - math.tan(math.radians(22.5)))
    pts = [(-w / 2 + c, -h / 2), (w / 2 - c, -h / 2), (w / 2, -h / 2 + c), (w / 2, h / 2 - c),
           (w / 2 - c, h / 2), (-w / 2 + c, h / 2), (-w / 2, h / 2 - c), (-w / 2, -h / 2 + c)]
    pts = [(x + yc, z + EYE_ZC) for (x, z) in pts]
    return (cq.Workplane("YZ").workplane(offset=EYE_X_START).polyline(pts).close()
            .extrude(20, taper=EYE_TAPER))


for yc in (-EYE_Y, EYE_Y):
    body = body.union(eye(yc).intersect(head_shape(EYE_UP)))


# ---------------- ears: octagonal hub + tapered blade, raised strap below ----------------
def octagon(wp, cx, cz, r):
    pts = [(cx + r * math.cos(math.radians(22.5 + 45 * i)),
            cz + r * math.sin(math.radians(22.5 + 45 * i))) for i in range(8)]
    return wp.polyline(pts).close()


# ear blade outline in the XZ plane (tip at the top rear, base on the hub)
BLADE_PTS = [(63.1, 107.9), (61.75, 104.6), (61.9, 98.8), (63.7, 95.3), (85.2, 59.0),
             (96.0, 52.0), (100.9, 62.4), (63.9, 107.8)]

for s in (-1, 1):
    # XZ workplane normal is -Y: offset the workplane along its normal
    y_in = s * ARM_Y0
    y_out = s * (ARM_Y0 + ARM_T)
    blade = (cq.Workplane("XZ").polyline(BLADE_PTS).close()
             .extrude(ARM_T).translate((0, max(y_in, y_out) + 0.0, 0)))
    hub = (octagon(cq.Workplane("XZ"), PIVOT_X, PIVOT_Z, HUB_R).extrude(HUB_T)
           .translate((0, max(s * (HW - 0.3), s * (HW - 0.3 + HUB_T)), 0)))
    washer = (octagon(cq.Workplane("XZ"), PIVOT_X, PIVOT_Z, HUB_R + 1.6).extrude(1.5)
              .translate((0, max(s * (HW - 0.3), s * (HW - 0.3 + 1.5)), 0)))
    body = body.union(blade).union(hub).union(washer)
    # small pivot pin hole
    pin = (cq.Workplane("XZ").center(PIVOT_X, PIVOT_Z).circle(0.8).extrude(2.0)
           .translate((0, max(s * (HW - 0.3 + HUB_T), s * (HW - 0.3 + HUB_T - 2.0)), 0)))
    body = body.cut(pin)

# raised straps running down from the hubs along the head sides
strap_prof = (cq.Workplane("XZ").polyline([(84.0, 52.0), (99.0, 52.0), (98.0, 13.0), (84.5, 6.0)])
              .close().extrude(BIG / 2, both=True))
strap = strap_prof.intersect(head_shape(0.0, STRAP_T))
body = body.union(strap)

# ---------------- carry handle on the lid ----------------
hz0 = lid_top_z(HANDLE_X0) - 2.0
handle = (cq.Workplane("YZ").center(0, (hz0 + HANDLE_TOP) / 2)
          .rect(2 * HANDLE_HY, HANDLE_TOP - hz0).extrude(HANDLE_W)
          .translate((HANDLE_X0, 0, 0)))
handle = handle.edges("|X and >Z").fillet(HANDLE_R)
inner = (cq.Workplane("YZ").center(0, hz0).rect(2 * (HANDLE_HY - HANDLE_LEG),
         2 * (HANDLE_TOP - HANDLE_BAR - hz0)).extrude(HANDLE_W).translate((HANDLE_X0, 0, 0)))
inner = inner.edges("|X and >Z").fillet(HANDLE_R - HANDLE_LEG + 0.5)
handle = handle.cut(inner)
handle = handle.cut(cq.Workplane("XZ").center(HANDLE_X0 + HANDLE_W / 2, hz0 + 6.0).circle(1.2)
                    .extrude(BIG / 2, both=True))
body = body.union(handle)

# ---------------- foot lug under the tunnel ----------------
foot = (cq.Workplane("XY").center(FOOT_X, 0).slot2D(2 * FOOT_HY, FOOT_W, 90).extrude(FOOT_H))
foot = foot.faces(">Z").edges().chamfer(1.2)
body = body.union(foot)
for s in (-1, 1):
    hexp = (cq.Workplane("XY").center(FOOT_X, s * (FOOT_HY - FOOT_W / 2)).polygon(6, 8.0)
            .extrude(3.0).translate((0, 0, FOOT_H - 3.0)))
    body = body.cut(hexp)

# small rectangular recess in the sloped bottom of the back box
rz = BACK_BOT_Z * (1 - 12.0 / BOT_FLAT_X0)
body = body.cut(cq.Workplane("XY").box(7.0, 9.0, 6.0).translate((12.0, 0, rz)))

# ---------------- round plate on the lid top in front of the head ----------------
dz = lid_top_z(DISC_X)
disc = cq.Workplane("XY").center(DISC_X, 0).circle(DISC_R).extrude(DISC_H + 3).translate((0, 0, dz - 3))
body = body.union(disc)

# ---------------- small holes on the lid top ----------------
for hx in (43.4, 72.3):
    for hy in (-18.75, 18.75):
        body = body.cut(cq.Workplane("XY").center(hx, hy).circle(0.9).extrude(6)
                        .translate((0, 0, lid_top_z(hx) - 5)))

# ---------------- pocket at the back of the lid ----------------
bp_x0, bp_x1, bp_hy, bp_d = 5.5, 34.0, 14.0, 3.5
bpocket = (cq.Workplane("XY").center((bp_x0 + bp_x1) / 2, 0).rect(bp_x1 - bp_x0, 2 * bp_hy)
           .extrude(20).translate((0, 0, LID_TOP_BACK - bp_d)))
body = body.cut(bpocket)
for (cx, cy, w, h) in ((20.0, 8.2, 7.5, 8.5), (20.0, -8.2, 7.5, 8.5), (13.0, 0.0, 5.8, 6.4)):
    body = body.union(cq.Workplane("XY").center(cx, cy).rect(w, h).extrude(2.0)
                      .translate((0, 0, LID_TOP_BACK - bp_d)))

# ---------------- shallow stepped panel on the back box sides ----------------
panel_side = (cq.Workplane("XZ")
              .polyline([(-1.0, 35.9), (8.5, 35.9), (11.0, 52.7), (14.8, 52.7), (17.9, 35.9),
                         (29.8, 17.8), (30.0, -1.0), (-1.0, -1.0)])
              .close().extrude(BIG / 2, both=True))
body = body.cut(panel_side.cut(plan_solid(SIDE_INSET + SIDE_PANEL_D)))

# ---------------- small slots low on the back box sides ----------------
for s in (-1, 1):
    yy = s * (BACK_HW + (HW - BACK_HW) / TAPER_X1 * 21.0 - SIDE_INSET)
    body = body.cut(cq.Workplane("XY").box(11.0, 3.0, 3.5).translate((21.0, yy, 20.3)))

# ---------------- grip slots on the lid sides ----------------
for s in (-1, 1):
    slot = (cq.Workplane("XY").box(GRIP_L, 10.0, GRIP_H)
            .translate((GRIP_X, s * (GRIP_Y + 5.0), GRIP_Z)))
    body = body.cut(slot)
    tab = (cq.Workplane("XY").box(GRIP_L * 0.45, 2.5, GRIP_H - 1.5)
           .translate((GRIP_X - GRIP_L * 0.18, s * (GRIP_Y + 1.25), GRIP_Z)))
    body = body.union(tab)

# ---------------- truss pockets on the tunnel back wall ----------------
tw_hy = 26.0
for s in (-1, 1):
    pk = (cq.Workplane("YZ").center(s * (tw_hy / 2 + 1.5), 33.0).rect(tw_hy - 3.0, 32.0)
          .extrude(3.5).translate((WIN_X0 - 3.5, 0, 0)))
    body = body.cut(pk)
    y0, y1 = s * 3.0, s * (tw_hy + 1.5)
    diag = (cq.Workplane("YZ").polyline([(y0, 17.0), (y0, 20.5), (y1, 49.0), (y1, 45.5)]).close()
            .extrude(3.5).translate((WIN_X0 - 3.5, 0, 0)))
    body = body.union(diag)
    hbar = (cq.Workplane("YZ").center(s * (tw_hy / 2 + 1.5), 40.0).rect(tw_hy - 3.0, 2.0)
            .extrude(3.5).translate((WIN_X0 - 3.5, 0, 0)))
    body = body.union(hbar)

# ---------------- round boss on the tunnel ceiling ----------------
body = body.union(cq.Workplane("XY").center(CEIL_X, 0).circle(CEIL_R).extrude(CEIL_H + 1.0)
                  .translate((0, 0, WIN_Z1 - CEIL_H)))

result = body
